import cadquery as cq

# =====================================================================
#  U-shaped mounting bracket with a thick, round-padded base
#  - two parallel side legs (X = +/-), rounded top corners, one hole each
#  - thick base with large inner / outer bend radii
#  - a round pad (disc) under the base that protrudes past both ends
#  - four through holes in the base (asymmetric "T/diamond" pattern)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 100.0        # outer width of the U (X)
D = 78.0         # depth of the U plate (Y)
H = 93.0         # overall height (Z)
T_LEG = 8.0      # leg (side wall) thickness
T_BOT = 15.4     # base thickness (inner floor height)
R_OUT = 22.0     # outer bend radius (base -> leg, outside)
R_IN = 23.0      # inner bend radius (floor -> leg, inside)
R_TOP = 15.0     # rounding of the leg top corners (seen from the side)

PAD_D = 86.0     # diameter of the round base pad (flush with floor & underside)

LEG_HOLE_D = 7.8     # hole through each leg
LEG_HOLE_Z = 60.5    # height of the leg-hole centre above the underside

BOT_HOLE_D = 8.0     # holes through the base
BOT_HOLES = [        # (x, y) centres
    (0.0, 19.5),
    (0.0, -19.5),
    (14.0, -2.6),
    (-14.0, -2.6),
]

# orientation of the (invisible) seam of the cylindrical hole faces
LEG_SEAM_DEG = 130.0
BOT_SEAM_DEG = 45.0

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def outer_prism(length):
    """Outer envelope of the U: a block with the two bottom long edges rounded."""
    return (
        cq.Workplane("XY")
        .box(W, length, H, centered=(True, True, False))
        .edges("|Y and <Z")
        .fillet(R_OUT)
    )


# ---------------- U body ----------------
body = outer_prism(D)

# open-topped cavity between the legs, floor at T_BOT, rounded inner bends
cavity = (
    cq.Workplane("XY")
    .box(W - 2 * T_LEG, D + 20.0, H + 10.0, centered=(True, True, False))
    .edges("|Y and <Z")
    .fillet(R_IN)
    .translate((0, 0, T_BOT))
)
body = body.cut(cavity)

# round the top corners of both legs (edges running along X at the top)
body = body.edges("|X and >Z").fillet(R_TOP)

# ---------------- round base pad ----------------
# disc under the floor, trimmed to the outer U envelope so it only shows
# where it sticks out past the two ends of the bracket
pad = cq.Workplane("XY").circle(PAD_D / 2.0).extrude(T_BOT)
pad = pad.intersect(outer_prism(PAD_D + 20.0))
body = body.union(pad)

# ---------------- holes ----------------
# one hole straight through both legs (along X), centred in Y
leg_hole = (
    cq.Workplane("YZ", origin=(-W, 0, LEG_HOLE_Z))
    .transformed(rotate=(0, 0, LEG_SEAM_DEG))
    .circle(LEG_HOLE_D / 2.0)
    .extrude(2.0 * W)
)
body = body.cut(leg_hole)

# four holes through the base
for (hx, hy) in BOT_HOLES:
    h = (
        cq.Workplane("XY", origin=(hx, hy, -5.0))
        .transformed(rotate=(0, 0, BOT_SEAM_DEG))
        .circle(BOT_HOLE_D / 2.0)
        .extrude(T_BOT + 10.0)
    )
    body = body.cut(h)

result = body
